import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
# base plate (origin = plate centre, plate bottom at z = 0)
PL_W = 105.5      # X
PL_D = 96.6       # Y
PL_T = 4.4        # thickness
PL_R = 3.0        # corner radius (plan view)
PL_FT = 1.8       # top edge fillet
PL_FB = 0.5       # bottom edge fillet

# stand-off posts (wire posts with bore and slits)
POST_X = -44.1
POST_Y = 41.9
POST_D = 7.9
POST_H = 21.5     # above plate top
POST_HOLE = 2.1
POST_SLIT = 0.45
POST_TOP_F = 0.4
POST_CB_D = 7.0   # shallow recess under each post
POST_CB_T = 0.8
FRONT_SLITS = (90.0, 235.0, 310.0)   # slit directions, post at -Y
BACK_SLITS = (10.0,)                  # slit directions, post at +Y
BACK_WIN_ANG = 30.0                  # wire exit window, post at +Y
BACK_WIN_W = 2.2
BACK_WIN_H = 9.0

# holes
CORNER_X = 44.4
HOLE_Y = 41.9
CORNER_HOLE = 2.8
CORNER_CSK = 5.4
SIDE_X = -34.0
SIDE_HOLE = 2.8
SIDE_CSK = 5.4
CENTER_HOLES = [(-19.0, 0.0), (28.4, 0.0)]
CENTER_HOLE = 1.9
CENTER_CSK_BOT = 3.6

# scribed wire-guide lines
GROOVE_W = 0.3
GROOVE_D = 0.3
LINE_END = (4.4, -37.5)

# label on top of plate
LABEL = "LRS-50-12 WELL"
LABEL_SIZE = 7.5
LABEL_DEPTH = 0.5
LABEL_POS = (4.85, -41.6)

# side bracket (U channel with slotted wall and flange)
BR_X0 = -89.9     # outer face of tall wall
BR_CH_W = 11.5    # channel width
BR_FL_W = 13.85   # flange width beyond channel
BR_FL_Y1 = 20.7   # flange ends at this Y (starts at -Y end)
BR_FL_R = 6.6     # flange corner radius
BR_L = 96.6       # length along Y
BR_H = 21.0       # overall height
BR_FLOOR = 2.7    # floor / flange thickness
BR_WALL = 1.35    # wall thickness
BR_END = 1.6      # end wall thickness
BR_OUT_R = 2.8    # outer corner radius
BR_IN_R = 1.6     # inner corner radius
BR_INSET = 0.15   # walls sit slightly inside the floor outline
BR_BOT_F = 0.4    # bottom edge rounding
BR_TAB_F = 0.9    # rounding of the tab tops
BR_HOLE = 2.1
BR_HOLE_X = -81.4
BR_HOLE_Y = 41.7
SLOT_N = 5
SLOT_W = 2.45
SLOT_PITCH = 7.83
SLOT_Y0 = -22.4   # centre of first slot
SLOT_FLOOR_GAP = 0.3
# terminal label under the bracket
BR_LABEL_SIZE = 6.5
BR_LABEL_POS = (-74.8, -8.35)
BR_LABEL_PITCH = 8.0


# ---------------- helpers ----------------
def wp_solid(s):
    return cq.Workplane("XY").add(s)


def groove(p0, p1, z_face, w=GROOVE_W, d=GROOVE_D):
    """thin straight groove between two points on a horizontal face at z_face"""
    (x0, y0), (x1, y1) = p0, p1
    L = math.hypot(x1 - x0, y1 - y0)
    ang = math.degrees(math.atan2(y1 - y0, x1 - x0))
    return (cq.Workplane("XY").box(L + w, w, d * 2)
            .rotate((0, 0, 0), (0, 0, 1), ang)
            .translate(((x0 + x1) / 2.0, (y0 + y1) / 2.0, z_face)))


def radial_cut(cx, cy, ang, width, r_out, z0, z1):
    """box from the post axis outwards along direction ang (deg)"""
    L = r_out + 0.5
    return (cq.Workplane("XY").box(L, width, z1 - z0)
            .translate((L / 2.0, 0, (z0 + z1) / 2.0))
            .rotate((0, 0, 0), (0, 0, 1), ang)
            .translate((cx, cy, 0)))


def csk_tool(x, y, d, dk, z_top):
    """through hole with a 90 deg countersink opening at z_top"""
    h = (dk - d) / 2.0
    cone = cq.Solid.makeCone(d / 2.0, dk / 2.0, h, pnt=cq.Vector(x, y, z_top - h),
                             dir=cq.Vector(0, 0, 1))
    cyl = cq.Solid.makeCylinder(d / 2.0, z_top + 2, pnt=cq.Vector(x, y, -1))
    cap = cq.Solid.makeCylinder(dk / 2.0, 1.0, pnt=cq.Vector(x, y, z_top))
    return wp_solid(cone).union(wp_solid(cyl)).union(wp_solid(cap))


# ---------------- base plate ----------------
plate = (cq.Workplane("XY").rect(PL_W, PL_D).extrude(PL_T)
         .edges("|Z").fillet(PL_R)
         .faces(">Z").edges().fillet(PL_FT)
         .faces("<Z").edges().fillet(PL_FB))

# posts
for sy in (1, -1):
    post = (cq.Workplane("XY").workplane(offset=PL_T - 0.01)
            .center(POST_X, sy * POST_Y).circle(POST_D / 2.0)
            .extrude(POST_H + 0.01)
            .faces(">Z").edges().fillet(POST_TOP_F))
    plate = plate.union(post)

# post bores, slits, exit window and under-side recesses
z_top = PL_T + POST_H
for sy, slits in ((1, BACK_SLITS), (-1, FRONT_SLITS)):
    cx, cy = POST_X, sy * POST_Y
    bore = wp_solid(cq.Solid.makeCylinder(POST_HOLE / 2.0, z_top + 2, pnt=cq.Vector(cx, cy, -1)))
    plate = plate.cut(bore)
    for a in slits:
        plate = plate.cut(radial_cut(cx, cy, a, POST_SLIT, POST_D / 2.0, PL_T + 0.05, z_top + 1))
    rec = wp_solid(cq.Solid.makeCylinder(POST_CB_D / 2.0, POST_CB_T + 0.01,
                                         pnt=cq.Vector(cx, cy, -0.01)))
    plate = plate.cut(rec)
plate = plate.cut(radial_cut(POST_X, POST_Y, BACK_WIN_ANG, BACK_WIN_W, POST_D / 2.0,
                             PL_T + 0.05, PL_T + BACK_WIN_H))

# countersunk holes from the top
for (x, y) in [(CORNER_X, HOLE_Y), (CORNER_X, -HOLE_Y)]:
    plate = plate.cut(csk_tool(x, y, CORNER_HOLE, CORNER_CSK, PL_T))
for (x, y) in [(SIDE_X, HOLE_Y), (SIDE_X, -HOLE_Y)]:
    plate = plate.cut(csk_tool(x, y, SIDE_HOLE, SIDE_CSK, PL_T))

# small centre holes, lightly countersunk from below
for (x, y) in CENTER_HOLES:
    h = (CENTER_CSK_BOT - CENTER_HOLE) / 2.0
    tool = (wp_solid(cq.Solid.makeCylinder(CENTER_HOLE / 2.0, PL_T + 2, pnt=cq.Vector(x, y, -1)))
            .union(wp_solid(cq.Solid.makeCone(CENTER_CSK_BOT / 2.0, CENTER_HOLE / 2.0, h,
                                              pnt=cq.Vector(x, y, 0), dir=cq.Vector(0, 0, 1))))
            .union(wp_solid(cq.Solid.makeCylinder(CENTER_CSK_BOT / 2.0, 1.0,
                                                  pnt=cq.Vector(x, y, -1.0)))))
    plate = plate.cut(tool)

# scribed wire-guide lines on top
top_path = [CENTER_HOLES[0], CENTER_HOLES[1], LINE_END]
for a, b in zip(top_path[:-1], top_path[1:]):
    plate = plate.cut(groove(a, b, PL_T))
plate = plate.cut(groove((POST_X, POST_Y), CENTER_HOLES[0], PL_T, w=0.2, d=0.15))
for sy in (1, -1):
    plate = plate.cut(groove((POST_X, sy * POST_Y), (SIDE_X, sy * POST_Y), PL_T))
    plate = plate.cut(groove((POST_X, sy * POST_Y), (-PL_W / 2.0 - 1.0, sy * (POST_Y + 3.6)), PL_T))
# scribed lines underneath
bot_path = [(SIDE_X, -HOLE_Y), CENTER_HOLES[1], CENTER_HOLES[0], (SIDE_X, -HOLE_Y)]
for a, b in zip(bot_path[:-1], bot_path[1:]):
    plate = plate.cut(groove(a, b, 0.0))
plate = plate.cut(groove((SIDE_X, HOLE_Y), (CORNER_X, HOLE_Y), 0.0))

# engraved label
try:
    txt = (cq.Workplane("XY").workplane(offset=PL_T)
           .text(LABEL, LABEL_SIZE, -LABEL_DEPTH, kind="bold",
                 font="DejaVu Sans", halign="center", valign="center")
           .translate((LABEL_POS[0], LABEL_POS[1], 0)))
    plate = plate.cut(txt)
except Exception:
    pass

# ---------------- side bracket ----------------
x_ch1 = BR_X0 + BR_CH_W
x_fl1 = x_ch1 + BR_FL_W
y0, y1 = -BR_L / 2.0, BR_L / 2.0

# floor + flange outline (plan)
base = (cq.Workplane("XY")
        .moveTo(BR_X0, y0)
        .lineTo(x_fl1, y0)
        .lineTo(x_fl1, BR_FL_Y1)
        .lineTo(x_ch1, BR_FL_Y1)
        .lineTo(x_ch1, y1)
        .lineTo(BR_X0, y1)
        .close()
        .extrude(BR_FLOOR))
base = base.edges("|Z").edges(cq.selectors.NearestToPointSelector((x_fl1, y0, 1))).fillet(BR_FL_R)
for yy in (y0, y1):
    base = (base.edges("|Z")
            .edges(cq.selectors.BoxSelector((BR_X0 - 1, yy - 1, -1), (BR_X0 + 1, yy + 1, BR_H + 1)))
            .fillet(BR_OUT_R))
try:
    base = base.faces("<Z").edges().fillet(BR_BOT_F)
except Exception:
    pass

# U walls: tall wall + two end walls, standing on the floor
e = BR_INSET
wx0, wy0, wy1, wx1 = BR_X0 + e, y0 + e, y1 - e, x_ch1 - e
walls = (cq.Workplane("XY").workplane(offset=BR_FLOOR - 0.5)
         .moveTo(wx0, wy0)
         .lineTo(wx1, wy0)
         .lineTo(wx1, y0 + BR_END)
         .lineTo(BR_X0 + BR_WALL, y0 + BR_END)
         .lineTo(BR_X0 + BR_WALL, y1 - BR_END)
         .lineTo(wx1, y1 - BR_END)
         .lineTo(wx1, wy1)
         .lineTo(wx0, wy1)
         .close()
         .extrude(BR_H - BR_FLOOR + 0.5))
for yy in (wy0, wy1):
    walls = (walls.edges("|Z")
             .edges(cq.selectors.BoxSelector((wx0 - 1, yy - 1, -1), (wx0 + 1, yy + 1, BR_H + 1)))
             .fillet(BR_OUT_R - e))
for yy in (y0 + BR_END, y1 - BR_END):
    xi = BR_X0 + BR_WALL
    walls = (walls.edges("|Z")
             .edges(cq.selectors.BoxSelector((xi - 0.1, yy - 0.1, -1), (xi + 0.1, yy + 0.1, BR_H + 1)))
             .fillet(BR_IN_R))
bracket = base.union(walls)

# slots in the tall wall
zb = BR_FLOOR + SLOT_FLOOR_GAP
for i in range(SLOT_N):
    yc = SLOT_Y0 + i * SLOT_PITCH
    s = (cq.Workplane("XY").box(BR_WALL * 4, SLOT_W, BR_H - zb + 1)
         .translate((BR_X0 + BR_WALL / 2.0, yc, zb + (BR_H - zb + 1) / 2.0)))
    bracket = bracket.cut(s)

# round the top corners of the tabs between the slots
try:
    bracket = (bracket.edges("|X")
               .edges(cq.selectors.BoxSelector((BR_X0 - 1, SLOT_Y0 - SLOT_PITCH, BR_H - 0.1),
                                               (BR_X0 + BR_WALL + 1,
                                                SLOT_Y0 + SLOT_N * SLOT_PITCH, BR_H + 0.1)))
               .fillet(BR_TAB_F))
except Exception:
    pass

# floor holes
for sy in (1, -1):
    bracket = bracket.cut(wp_solid(cq.Solid.makeCylinder(
        BR_HOLE / 2.0, BR_FLOOR + 2, pnt=cq.Vector(BR_HOLE_X, sy * BR_HOLE_Y, -1))))

# scribed lines along the floor / flange
bracket = bracket.cut(groove((BR_HOLE_X, -BR_HOLE_Y), (BR_HOLE_X, BR_HOLE_Y), BR_FLOOR, w=0.2, d=0.2))
bracket = bracket.cut(groove((x_ch1, y0 + 3.0), (x_ch1, BR_FL_Y1), BR_FLOOR, w=0.2, d=0.2))
bracket = bracket.cut(groove((x_ch1 + 6.7, y0 + 3.0), (x_ch1 + 6.7, BR_FL_Y1 - 0.3), BR_FLOOR,
                             w=0.2, d=0.2))

# terminal marking engraved on the underside: "L N (earth) - +"
BR_LABEL_Y = [BR_LABEL_POS[1] + (i - 2) * BR_LABEL_PITCH for i in range(5)]
s = BR_LABEL_SIZE
for ch, yy in zip(("L", "N", None, "-", "+"), BR_LABEL_Y):
    if ch is None:
        # earth symbol built from bars (glyph "up" = +X)
        ex = BR_LABEL_POS[0]
        t = 0.12 * s
        for dx, L in ((0.0, 0.62 * s), (-0.17 * s, 0.42 * s), (-0.34 * s, 0.22 * s)):
            bracket = bracket.cut(cq.Workplane("XY").box(t, L, 0.8).translate((ex + dx, yy, 0)))
        bracket = bracket.cut(cq.Workplane("XY").box(0.32 * s, t, 0.8)
                              .translate((ex + 0.16 * s, yy, 0)))
        continue
    try:
        under = cq.Plane(origin=(BR_LABEL_POS[0], yy, 0), xDir=(0, 1, 0), normal=(0, 0, -1))
        g = cq.Workplane(under).text(ch, s, -0.4, kind="bold", font="DejaVu Sans",
                                     halign="center", valign="center")
        bracket = bracket.cut(g)
    except Exception:
        pass

result = plate.union(bracket)

VIEW = {"azimuth": 45, "elevation": 26}
